import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
D = 100.0            # outer diameter of the cap
R = D / 2.0
T = 19.2             # body thickness (front face -> rim back face)
LIP_H = 0.4          # small raised lip on the rim back face
R_LIP = 46.0         # outer radius of the raised lip
R_REC = 45.0         # radius of the back recess
REC_DEPTH = 9.5      # depth of the back recess (from rim back face)
F_FRONT = 1.5        # fillet on the front outer edge
F_BACK = 1.7         # fillet on the back outer edge
F_FLOOR = 1.5        # fillet between recess wall and floor
F_LIP = 0.5          # rounding of the lip's inner edge

SLOT_W = 42.7        # straight slot
SLOT_H = 6.1
SLOT_Z = 2.0

MOUTH_R = 30.3       # smile: circular segment below a chord
MOUTH_CHORD_Z = -16.9
MOUTH_FILLET = 3.7   # rounded top (chord) edges of the smile

PIN_X = 16.3         # two pins ("eyes") on the recess floor
PIN_Z = 25.2
PIN_D = 3.8
PIN_L = 6.2
PIN_TIP_F = 1.5      # rounding of the pin tips
PIN_BASE_F = 0.5     # fillet at the pin roots

# Disc axis along Y: front face at y = -T (faces -Y), rim back at y = 0.


def arc_pts(cx, cy, r, a0, a1):
    """start, mid and end point of a circular arc (angles in degrees)."""
    am = 0.5 * (a0 + a1)
    p = lambda a: (cx + r * math.cos(math.radians(a)), cy + r * math.sin(math.radians(a)))
    return p(a0), p(am), p(a1)


# ---- revolved body profile in the (radius, axial) plane: X = radius, Y = axis ----
s = cq.Workplane("XY").moveTo(0, -T)
s = s.lineTo(R - F_FRONT, -T)
_, m, e = arc_pts(R - F_FRONT, -T + F_FRONT, F_FRONT, -90, 0)
s = s.threePointArc(m, e)
s = s.lineTo(R, -F_BACK)
_, m, e = arc_pts(R - F_BACK, -F_BACK, F_BACK, 0, 90)
s = s.threePointArc(m, e)
s = s.lineTo(R_LIP, 0)
s = s.lineTo(R_LIP, LIP_H)
s = s.lineTo(R_REC + F_LIP, LIP_H)
_, m, e = arc_pts(R_REC + F_LIP, LIP_H - F_LIP, F_LIP, 90, 180)
s = s.threePointArc(m, e)
s = s.lineTo(R_REC, -REC_DEPTH + F_FLOOR)
_, m, e = arc_pts(R_REC - F_FLOOR, -REC_DEPTH + F_FLOOR, F_FLOOR, 0, -90)
s = s.threePointArc(m, e)
s = s.lineTo(0, -REC_DEPTH)
s = s.close()
body = s.revolve(360, (0, 0, 0), (0, 1, 0))
# turn the revolve seam to the underside (cosmetic only)
body = body.rotate((0, 0, 0), (0, 1, 0), 135)

# ---- straight slot through the plate ----
slot = (
    cq.Workplane("XZ", origin=(0, 5, 0))
    .center(0, SLOT_Z)
    .rect(SLOT_W, SLOT_H)
    .extrude(T + 10)
)
body = body.cut(slot)

# ---- smile: circular segment below a chord, through the plate ----
half = math.sqrt(MOUTH_R ** 2 - MOUTH_CHORD_Z ** 2)
mouth = (
    cq.Workplane("XZ", origin=(0, 5, 0))
    .moveTo(-half, MOUTH_CHORD_Z)
    .lineTo(half, MOUTH_CHORD_Z)
    .threePointArc((0, -MOUTH_R), (-half, MOUTH_CHORD_Z))
    .close()
    .extrude(T + 10)
)
body = body.cut(mouth)


class ChordSel(cq.Selector):
    """the two straight chord edges of the smile (front face and recess floor)."""

    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() != "LINE":
                continue
            a, b = e.startPoint(), e.endPoint()
            if (abs(a.z - MOUTH_CHORD_Z) < 1e-3 and abs(b.z - MOUTH_CHORD_Z) < 1e-3
                    and abs(a.y - b.y) < 1e-6 and abs(a.x - b.x) > 1.0):
                out.append(e)
        return out


body = body.edges(ChordSel()).fillet(MOUTH_FILLET)

# ---- two pins on the recess floor ----
floor_y = -REC_DEPTH
for sx in (-1, 1):
    pin = (
        cq.Workplane("XZ", origin=(0, floor_y - 0.5, 0))
        .center(sx * PIN_X, PIN_Z)
        .circle(PIN_D / 2)
        .extrude(-(PIN_L + 0.5))
        .faces(">Y")
        .edges()
        .fillet(PIN_TIP_F)
    )
    body = body.union(pin)


class PinRootSel(cq.Selector):
    def filter(self, objs):
        out = []
        for e in objs:
            if e.geomType() != "CIRCLE":
                continue
            c = e.Center()
            if abs(c.y - floor_y) < 0.05 and abs(e.radius() - PIN_D / 2) < 1e-3:
                out.append(e)
        return out


body = body.edges(PinRootSel()).fillet(PIN_BASE_F)

result = body

VIEW = {"azimuth": 45, "elevation": 26}
